import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 46.0          # overall width  (X)
L = 78.0          # overall length (Y)
T = 9.4           # base plate thickness
H_WALL = 24.6     # height of walls / boss (from bottom)
H_PIL = 40.0      # pillar height (from bottom)

# plate outline
X_RF = 41.4       # right edge of the front part of the plate
DIAG_SLOPE = 0.385
R_PC = 8.3        # plate outline radius around the pillar (front-left)
CH_ANG = 49.0     # angle of the short bevel edge left of the pillar (deg)
D_BEV = 9.0       # distance of that bevel edge from the pillar axis
R_BEV = 1.0       # small round between left edge and bevel
R_FR = 7.5        # front-right corner radius
R_BL = 5.7        # back-left corner radius (plate)
R_BR = 1.5        # back-right corner radius
R_STEP_IN = 3.0   # concave corner between plate side and boss round
R_EDGE = 2.5      # plate top edge fillet
CH_BOT = 0.5      # bottom edge chamfer
CH_POCKET = 0.7   # chamfer on open edge of pocket floor
R_POCKET_V = 1.2  # rounds on vertical edges at the pocket opening

# pillar
PIL_X, PIL_Y = 10.9, 8.3
PIL_D = 13.0
PIL_FIL = 3.0

# walls (L shape: thick left wall + thin back wall)
WL_X0 = 3.6       # outer (-X) face of left wall
WL_X1 = 22.0      # inner face of left wall
WB_T = 5.4        # back wall thickness
WF_Y = 51.5       # front face of left wall (flat part, outer side)
WF_ARC_C = (9.0, 35.3)   # centre of the concave front sweep
R_WBL = 6.2       # back-left vertical edge radius of wall
R_WFO = 5.0       # front-outer rounded corner of left wall
R_WFI = 1.0       # front-inner rounded corner of left wall
BASE_FIL_WALL = 1.5   # blend between left wall and plate top
BASE_FIL_BOSS = 1.5   # blend between boss and plate top

# shallow vertical groove in the inner face of the left wall
NOTCH_Y = 66.8
NOTCH_R = 4.4
NOTCH_DEPTH = 1.6
NOTCH_EDGE_R = 0.8

# boss in front of the pocket
BOSS_X0 = 30.4
BOSS_Y1 = 43.3      # back face of boss (front of pocket)
BF_Y0 = 34.1        # slanted boss front face: y at x = BOSS_X0
BF_Y1 = 28.64       # slanted boss front face: y at x = W (before rounding)
R_BOSS = 6.3        # large front-right round of the boss
R_BOSS_BR = 0.5     # back-right vertical edge of the boss
R_BOSS_FL = 2.0     # front-left round of the boss

# holes
HOLE_SMALL_D = 4.8
SMALL_TOP_CH = 0.3
BOT_CB_D = 10.5
BOT_CB_DEPTH = 5.0
CB_D_C = 14.4        # counterbore of hole C
CB_D_E = 13.2        # counterbore of hole E
CB_DEPTH = 3.0
CB_HOLE_D = 7.2
CB_TOP_CH = 0.3
POCKET_HOLE_D = 7.9
HOLE_CH = 0.5

HOLE_A = (10.8, 59.9)   # wall top hole
HOLE_C = (10.5, 38.3)   # counterbored (top)
HOLE_E = (29.6, 19.3)   # counterbored (top)
HOLE_D = (36.8, 38.4)   # boss hole
HOLE_B = (31.5, 57.8)   # pocket floor hole

TEXT = "V1.1.4"
TEXT_SIZE = 5.8
TEXT_SX = 0.86      # horizontal condensing of the lettering
TEXT_DEPTH = 0.5
TEXT_X = 34.0
TEXT_Z = 17.1


# ---------------- helpers ----------------
def fillet_face(face, corners):
    """corners: list of ((x, y), r) -> fillet2D on the vertex nearest (x, y)."""
    for (x, y), r in corners:
        if r <= 0:
            continue
        v = min(face.Vertices(), key=lambda v: (v.X - x) ** 2 + (v.Y - y) ** 2)
        face = face.fillet2D(r, [v])
    return face


def poly_face(pts):
    w = cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True)
    return cq.Face.makeFromWires(w)


def prism(face, z0, z1):
    f = face.translate(cq.Vector(0, 0, z0))
    return cq.Solid.extrudeLinear(f, cq.Vector(0, 0, z1 - z0))


def revolve_cutter(profile, x, y):
    """profile: list of (r, z) points (closed polygon touching axis r=0)."""
    wp = cq.Workplane("XZ").polyline(profile).close()
    solid = wp.revolve(360, (0, 0, 0), (0, 1, 0)).val()
    return solid.translate(cq.Vector(x, y, 0))


# ---------------- boss footprint ----------------
boss_face = fillet_face(poly_face([
    (BOSS_X0, BOSS_Y1), (BOSS_X0, BF_Y0), (W, BF_Y1), (W, BOSS_Y1)]), [
    ((BOSS_X0, BF_Y0), R_BOSS_FL),
    ((W, BF_Y1), R_BOSS),
    ((W, BOSS_Y1), R_BOSS_BR),
])

# ---------------- base plate ----------------
# front-left: left edge -> short bevel -> arc around the pillar -> diagonal
def _line_isect(p1, d1, p2, d2):
    den = d1[0] * d2[1] - d1[1] * d2[0]
    t = ((p2[0] - p1[0]) * d2[1] - (p2[1] - p1[1]) * d2[0]) / den
    return (p1[0] + t * d1[0], p1[1] + t * d1[1])


a_b = math.radians(CH_ANG)
n_bev = (-math.sin(a_b), -math.cos(a_b))          # outward normal of bevel
d_bev = (math.cos(a_b), -math.sin(a_b))
t_bev = (PIL_X + D_BEV * n_bev[0], PIL_Y + D_BEV * n_bev[1])
dn = math.hypot(1.0, DIAG_SLOPE)
d_dia = (1.0 / dn, DIAG_SLOPE / dn)
n_dia = (DIAG_SLOPE / dn, -1.0 / dn)               # outward normal of diagonal
t_dia = (PIL_X + R_PC * n_dia[0], PIL_Y + R_PC * n_dia[1])
p_lb = _line_isect((0.0, 0.0), (0.0, 1.0), t_bev, d_bev)      # left edge / bevel
p_bd = _line_isect(t_bev, d_bev, t_dia, d_dia)                # bevel / diagonal
p_dr = _line_isect(t_dia, d_dia, (X_RF, 0.0), (0.0, 1.0))     # diagonal / right
plate_pts = [
    p_lb,
    p_bd,
    p_dr,
    (X_RF, BOSS_Y1 - 9.0),     # step hidden inside the boss footprint
    (W, BOSS_Y1 - 4.0),
    (W, L),
    (0.0, L),
]
plate_face = fillet_face(poly_face(plate_pts), [
    (p_bd, R_PC),
    (p_lb, R_BEV),
    (p_dr, R_FR),
    ((W, L), R_BR),
    ((0.0, L), R_BL),
])
plate_face = plate_face.fuse(boss_face).clean().Faces()[0]
# concave corner where the plate side meets the boss round
junction_y = max((v for v in plate_face.Vertices() if abs(v.X - X_RF) < 1e-3),
                 key=lambda v: v.Y).Y
plate_face = fillet_face(plate_face, [((X_RF, junction_y), R_STEP_IN)])
plate = prism(plate_face, 0, T)
# round the top outer edges of the plate
top_edges = [e for e in plate.Edges() if abs(e.Center().z - T) < 1e-6]
plate = plate.fillet(R_EDGE, top_edges)

# ---------------- walls (left + back, L shape) ----------------
ax, ay = WF_ARC_C
ar = WF_Y - ay
y_in = ay + math.sqrt(ar ** 2 - (WL_X1 - ax) ** 2)      # arc meets inner face
a0 = math.pi / 2
a1 = math.atan2(y_in - ay, WL_X1 - ax)
am = 0.5 * (a0 + a1)
wall_wire = (cq.Workplane("XY")
             .moveTo(WL_X0, WF_Y)
             .lineTo(ax, WF_Y)
             .threePointArc((ax + ar * math.cos(am), ay + ar * math.sin(am)),
                            (WL_X1, y_in))
             .lineTo(WL_X1, L - WB_T)
             .lineTo(W, L - WB_T)
             .lineTo(W, L)
             .lineTo(WL_X0, L)
             .close()
             .wire().val())
wall_face = cq.Face.makeFromWires(wall_wire)
wall_face = fillet_face(wall_face, [
    ((WL_X0, WF_Y), R_WFO),
    ((WL_X1, y_in), R_WFI),
    ((W, L - WB_T), R_POCKET_V),
    ((WL_X1, L - WB_T), 0.5),
    ((W, L), R_BR),
    ((WL_X0, L), R_WBL),
])
walls = prism(wall_face, 0, H_WALL)

boss = prism(boss_face, 0, H_WALL)

# ---------------- pillar ----------------
pillar = cq.Solid.makeCylinder(PIL_D / 2, H_PIL - 1.0,
                               cq.Vector(PIL_X, PIL_Y, 1.0))
# turn the seam of the cylinder towards the back (+Y)
pillar = pillar.rotate(cq.Vector(PIL_X, PIL_Y, 0), cq.Vector(PIL_X, PIL_Y, 1), 90)

# filler under the pocket keeps the open pocket edge sharp (it gets a
# small chamfer later instead of the plate's round)
filler = prism(poly_face([(WL_X1, BOSS_Y1 - 1.0), (W, BOSS_Y1 - 1.0),
                          (W, L - WB_T + 1.0), (WL_X1, L - WB_T + 1.0)]), 0, T)

body = plate.fuse(walls).fuse(boss).fuse(pillar).fuse(filler).clean()

# ---------------- fillet at the pillar base ----------------
pil_face = [f for f in body.Faces() if f.geomType() == "CYLINDER"
            and abs(f.Center().x - PIL_X) < 0.5 and abs(f.Center().y - PIL_Y) < 0.5
            and f.BoundingBox().zmax > H_PIL - 1][0]
pil_edges = [e for e in pil_face.Edges() if e.BoundingBox().zmax < T + 0.5]
try:
    body = body.fillet(PIL_FIL, pil_edges)
except Exception as ex:
    print("pillar fillet failed", ex)


# ---------------- blends at the base of the walls and boss ----------------
def wall_base_edges(shape):
    """Concave edges where the outside of the walls / boss meet the plate."""
    out = []
    for f in shape.Faces():
        bb = f.BoundingBox()
        if bb.zmax < T + 2 or bb.zmin > T + 1e-3:
            continue
        if f.geomType() not in ("PLANE", "CYLINDER"):
            continue
        if abs(f.normalAt(f.Center()).z) > 1e-3:
            continue
        for e in f.Edges():
            eb = e.BoundingBox()
            if abs(eb.zmin - T) > 1e-4 or abs(eb.zmax - T) > 1e-4:
                continue
            c = e.Center()
            if c.x > WL_X1 - 0.05 and c.y > BOSS_Y1 - 0.6:
                continue            # inside the pocket: keep sharp
            if c.y > L - WB_T - 0.5:
                continue            # back corner
            if math.hypot(c.x - PIL_X, c.y - PIL_Y) < PIL_D:
                continue            # pillar handled above
            out.append(e)
    return out


def safe_fillet(shape, r, edges, label=""):
    if not edges:
        return shape
    try:
        res = shape.fillet(r, edges)
        if res.isValid():
            return res
        print("fillet invalid, skipped", label)
    except Exception as ex:
        print("fillet failed", label, ex)
    return shape


# shallow vertical groove in the inner face of the left wall (cut before
# the blends so that the wall blend stops at the groove)
notch_cx = WL_X1 + NOTCH_R - NOTCH_DEPTH
body = body.cut(cq.Solid.makeCylinder(NOTCH_R, H_WALL,
                                      cq.Vector(notch_cx, NOTCH_Y, T))).clean()

be = wall_base_edges(body)
body = safe_fillet(body, BASE_FIL_WALL,
                   [e for e in be if e.Center().x < WL_X1 + 0.5], 'wall base')
be = wall_base_edges(body)
body = safe_fillet(body, BASE_FIL_BOSS,
                   [e for e in be if e.Center().x > BOSS_X0 - 0.5], 'boss base')

# soften the two vertical edges of the groove
notch_edges = [e for e in body.Edges() if e.geomType() == "LINE"
               and abs(e.Center().x - WL_X1) < 1e-3
               and abs(e.Center().y - NOTCH_Y) < NOTCH_R + 0.1
               and e.BoundingBox().zlen > 5]
body = safe_fillet(body, NOTCH_EDGE_R, notch_edges, 'notch edges')

# ---------------- holes ----------------
def hole_top_botcb(x, y, z_top):
    r1 = HOLE_SMALL_D / 2
    r2 = BOT_CB_D / 2
    c = HOLE_CH
    ct = SMALL_TOP_CH
    prof = [(0, -1), (r2 + c + 1, -1), (r2, c), (r2, BOT_CB_DEPTH),
            (r1, BOT_CB_DEPTH), (r1, z_top - ct), (r1 + ct + 1, z_top + 1),
            (0, z_top + 1)]
    return revolve_cutter(prof, x, y)


def hole_cbore_top(x, y, d_cb):
    rh = CB_HOLE_D / 2
    rc = d_cb / 2
    c = HOLE_CH
    ct = CB_TOP_CH
    zf = T - CB_DEPTH
    prof = [(0, -1), (rh + c + 1, -1), (rh, c), (rh, zf - ct), (rh + ct, zf),
            (rc, zf), (rc, T - ct), (rc + ct + 1, T + 1), (0, T + 1)]
    return revolve_cutter(prof, x, y)


def hole_plain(x, y, d, z_top):
    r = d / 2
    c = CB_TOP_CH
    prof = [(0, -1), (r + c + 1, -1), (r, c), (r, z_top - c),
            (r + c + 1, z_top + 1), (0, z_top + 1)]
    return revolve_cutter(prof, x, y)


cutters = [
    hole_top_botcb(PIL_X, PIL_Y, H_PIL),
    hole_top_botcb(HOLE_A[0], HOLE_A[1], H_WALL),
    hole_top_botcb(HOLE_D[0], HOLE_D[1], H_WALL),
    hole_cbore_top(HOLE_C[0], HOLE_C[1], CB_D_C),
    hole_cbore_top(HOLE_E[0], HOLE_E[1], CB_D_E),
    hole_plain(HOLE_B[0], HOLE_B[1], POCKET_HOLE_D, T),
]
for ct in cutters:
    body = body.cut(ct)
body = body.clean()

# ---------------- small chamfer on the open pocket edge ----------------
wedge_y0 = BOSS_Y1 - R_BOSS_BR
wedge_y1 = L - WB_T + R_POCKET_V
wedge = (cq.Workplane("XZ", origin=(0, wedge_y0, 0))
         .polyline([(W - CH_POCKET, T), (W, T - CH_POCKET), (W + 1, T + 1)])
         .close()
         .extrude(-(wedge_y1 - wedge_y0))
         .val())
body = body.cut(wedge).clean()

# ---------------- rounded vertical edge: boss back-left ----------------
def vertical_edge_at(shape, x, y, tol=0.05):
    return [e for e in shape.Edges() if e.geomType() == "LINE"
            and e.BoundingBox().zlen > 5 and e.BoundingBox().xlen < 1e-3
            and e.BoundingBox().ylen < 1e-3
            and abs(e.Center().x - x) < tol and abs(e.Center().y - y) < tol]


body = safe_fillet(body, R_POCKET_V, vertical_edge_at(body, BOSS_X0, BOSS_Y1), 'boss back-left')

# ---------------- bottom edge chamfer ----------------
bot = min(body.Faces(), key=lambda f: f.Center().z)
try:
    body = body.chamfer(CH_BOT, None, bot.outerWire().Edges())
except Exception as ex:
    print("bottom chamfer failed", ex)

result = cq.Workplane("XY").add(body)

# ---------------- engraved version text on back wall inner face ----------
def engraved_text(shape):
    """Bold sans text, slightly condensed in X, cut into the back wall."""
    from OCP.gp import gp_GTrsf, gp_Mat, gp_XYZ
    from OCP.BRepBuilderAPI import BRepBuilderAPI_GTransform
    pl = cq.Plane(origin=(TEXT_X, L - WB_T - 0.05, TEXT_Z), xDir=(1, 0, 0),
                  normal=(0, -1, 0))
    txt = (cq.Workplane(pl)
           .text(TEXT, TEXT_SIZE, -(TEXT_DEPTH + 0.05), combine=False,
                 font="DejaVu Sans", kind="bold")
           .vals())
    txt = cq.Compound.makeCompound(txt)
    g = gp_GTrsf()
    g.SetVectorialPart(gp_Mat(TEXT_SX, 0, 0, 0, 1, 0, 0, 0, 1))
    g.SetTranslationPart(gp_XYZ(TEXT_X * (1 - TEXT_SX), 0, 0))
    txt = cq.Shape.cast(BRepBuilderAPI_GTransform(txt.wrapped, g, True).Shape())
    return shape.cut(txt)


try:
    result = cq.Workplane("XY").add(engraved_text(result.val()))
except Exception as ex:
    print("text failed", ex)
